import math
import cadquery as cq

# ---------------------------------------------------------------
# Body 1 : chassis / base shell (open bottom)
# ---------------------------------------------------------------
B_L = 100.0      # length along X
B_W = 70.0       # width along Y
B_H = 21.0       # height
B_CX = 21.5      # chamfer run along X at the +X end
B_CY = 13.5      # chamfer run along Y at the +X end
B_T = 1.6        # wall thickness
B_TOP = 2.0      # top plate thickness

B_SIDE_HOLE_D = 9.3
B_SIDE_HOLE_X = (56.0, 69.0)          # holes in -Y and +Y walls
B_END_HOLE_D = 9.5
B_END_HOLE_SPACING = 13.0
B_PX_HOLE_YOFF = 1.5                  # +X end holes centre offset from mid
B_NX_HOLE_YOFF = -1.3                 # -X end holes centre offset from mid
B_HOLE_Z = 10.0

B_SLOT_LONG = (8.3, 47.3, 4.1, 12.1)  # x0, x1, y0, y1 (front slot, mirrored)
B_SLOT_END = (75.8, 83.6, 22.8, 47.2) # slot near +X end
B_MOUNT_D = 3.4
B_MOUNT_PTS = [(20.8, 17.0), (68.2, 17.0), (20.8, 53.0), (68.2, 53.0)]
B_BOSS_D = 5.5
B_BOSS_H = 1.5

# ---------------------------------------------------------------
# Body 2 : "mouse head" cover shell (open bottom)
# ---------------------------------------------------------------
M_X0, M_Y0, M_Z0 = 8.0, 97.3, -1.0   # placement of the cover
M_L = 81.5
M_W = 46.0
M_H = 30.4
M_TOPLEN = 54.5          # length of flat top before the slanted face
M_CX = 17.5              # footprint chamfer run along X
M_CY = 11.25             # footprint chamfer run along Y
M_T = 1.6                # wall thickness
M_SWITCH_D = 12.0
M_SWITCH_X = 20.2
M_SCREW_D = 4.0
M_SCREW_X = (12.0, 59.4)
M_SCREW_YIN = 5.0
M_SCREW_CB = 3.0         # depth of the clearance hole from the surface
M_TUBE_OD = 5.2
M_TUBE_ID = 1.8
M_TUBE_BOTTOM = 6.5
ENGRAVE = 0.5

# ===============================================================
# Base
# ===============================================================
base_pts = [(0, 0), (B_L - B_CX, 0), (B_L, B_CY), (B_L, B_W - B_CY),
            (B_L - B_CX, B_W), (0, B_W)]
base_outer = cq.Workplane("XY").polyline(base_pts).close().extrude(B_H)
base_inner = (cq.Workplane("XY").workplane(offset=-1.0)
              .polyline(base_pts).close().offset2D(-B_T, "intersection")
              .extrude(B_H - B_TOP + 1.0))
base = base_outer.cut(base_inner)

# bosses under the mounting holes
for (px, py) in B_MOUNT_PTS:
    boss = (cq.Workplane("XY").workplane(offset=B_H - B_TOP - B_BOSS_H)
            .center(px, py).circle(B_BOSS_D / 2).extrude(B_BOSS_H + 0.5))
    base = base.union(boss)

# mounting holes
for (px, py) in B_MOUNT_PTS:
    h = (cq.Workplane("XY").workplane(offset=B_H - B_TOP - B_BOSS_H - 1)
         .center(px, py).circle(B_MOUNT_D / 2).extrude(B_TOP + B_BOSS_H + 2))
    base = base.cut(h)

# slots in top plate
def slot_cut(x0, x1, y0, y1):
    return (cq.Workplane("XY").workplane(offset=B_H - B_TOP - 1)
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(x1 - x0, y1 - y0).extrude(B_TOP + 2))

sx0, sx1, sy0, sy1 = B_SLOT_LONG
base = base.cut(slot_cut(sx0, sx1, sy0, sy1))
base = base.cut(slot_cut(sx0, sx1, B_W - sy1, B_W - sy0))
base = base.cut(slot_cut(*B_SLOT_END))

# holes in -Y / +Y walls
for hx in B_SIDE_HOLE_X:
    cyl = (cq.Workplane("XZ", origin=(0, 5.0, 0)).center(hx, B_HOLE_Z)
           .circle(B_SIDE_HOLE_D / 2).extrude(10.0))
    base = base.cut(cyl)
    cyl = (cq.Workplane("XZ", origin=(0, B_W + 5.0, 0)).center(hx, B_HOLE_Z)
           .circle(B_SIDE_HOLE_D / 2).extrude(10.0))
    base = base.cut(cyl)

# holes in +X / -X end walls
for s in (-1, 1):
    yp = B_W / 2 + B_PX_HOLE_YOFF + s * B_END_HOLE_SPACING / 2
    cyl = (cq.Workplane("YZ", origin=(B_L - 5.0, 0, 0)).center(yp, B_HOLE_Z)
           .circle(B_END_HOLE_D / 2).extrude(10.0))
    base = base.cut(cyl)
    yn = B_W / 2 + B_NX_HOLE_YOFF + s * B_END_HOLE_SPACING / 2
    cyl = (cq.Workplane("YZ", origin=(-5.0, 0, 0)).center(yn, B_HOLE_Z)
           .circle(B_END_HOLE_D / 2).extrude(10.0))
    base = base.cut(cyl)

# ===============================================================
# Mouse head cover (built at local origin, moved afterwards)
# ===============================================================
M_RUN = M_L - M_TOPLEN
foot = [(0, 0), (M_L - M_CX, 0), (M_L, M_CY), (M_L, M_W - M_CY),
        (M_L - M_CX, M_W), (0, M_W)]

def head_solid(inset, z_lo, z_hi):
    """Chamfered footprint prism intersected with the slanted XZ profile,
    shrunk inward by `inset` (walls and slanted roof)."""
    fp = (cq.Workplane("XY").workplane(offset=z_lo)
          .polyline(foot).close())
    if inset > 0:
        fp = fp.offset2D(-inset, "intersection")
    prism = fp.extrude(z_hi - z_lo)
    # XZ side profile: slanted face from (M_TOPLEN, M_H) down to (M_L, 0)
    zb = -10.0
    xb = M_L + (0 - zb) * M_RUN / M_H
    # shift slanted line inward by inset along its normal
    nlen = math.hypot(M_H, M_RUN)
    dx = inset * nlen / M_H          # horizontal shift of a line with that slope
    prof = [(-10, zb), (xb - dx, zb), (M_TOPLEN - dx, M_H), (-10, M_H)]
    side = (cq.Workplane("XZ", origin=(0, M_W + 10, 0)).polyline(prof).close()
            .extrude(M_W + 20))
    return prism.intersect(side)

head_outer = head_solid(0.0, 0.0, M_H)
head_inner = head_solid(M_T, -1.0, M_H - M_T)
head = head_outer.cut(head_inner)

# slanted-face helper
def slant_z(x):
    """z of the outer slanted face at local x"""
    return M_H - (x - M_TOPLEN) * M_H / M_RUN

screw_pts = [(M_SCREW_X[0], M_SCREW_YIN), (M_SCREW_X[0], M_W - M_SCREW_YIN),
             (M_SCREW_X[1], M_SCREW_YIN), (M_SCREW_X[1], M_W - M_SCREW_YIN)]

# screw tubes (standoffs) from the roof down
for (px, py) in screw_pts:
    ztop = M_H if px <= M_TOPLEN else slant_z(px)
    tube = (cq.Workplane("XY").workplane(offset=M_TUBE_BOTTOM)
            .center(px, py).circle(M_TUBE_OD / 2)
            .extrude(M_H + 1.0 - M_TUBE_BOTTOM))
    head = head.union(tube)

# clip anything poking through the outer skin
head = head.intersect(head_outer)

for (px, py) in screw_pts:
    ztop = M_H if px <= M_TOPLEN else slant_z(px)
    # clearance counterbore through the roof into the top of the post
    hole = (cq.Workplane("XY").workplane(offset=ztop - M_SCREW_CB)
            .center(px, py).circle(M_SCREW_D / 2).extrude(M_SCREW_CB + 5))
    head = head.cut(hole)
    bore = (cq.Workplane("XY").workplane(offset=M_TUBE_BOTTOM - 1)
            .center(px, py).circle(M_TUBE_ID / 2).extrude(M_H))
    head = head.cut(bore)

# power switch hole
sw = (cq.Workplane("XY").workplane(offset=M_H - 5)
      .center(M_SWITCH_X, M_W / 2).circle(M_SWITCH_D / 2).extrude(10))
head = head.cut(sw)

# engraved lettering on the top (reads from the -X end, letters point +X)
def text_cut(txt, size, xc):
    t = (cq.Workplane(cq.Plane(origin=(xc, M_W / 2, M_H - ENGRAVE),
                               xDir=(0, -1, 0), normal=(0, 0, 1)))
         .text(txt, size, ENGRAVE + 1.0, kind="bold", halign="center",
               valign="center"))
    return t

try:
    head = head.cut(text_cut("MAZE", 6.6, 48.0))
    head = head.cut(text_cut("RUNNER", 6.2, 40.6))
    head = head.cut(text_cut("ON / OFF", 3.7, 29.8))
except Exception:
    pass

# mouse face engraving on the slanted face
nlen = math.hypot(M_H, M_RUN)
n_vec = (M_H / nlen, 0.0, M_RUN / nlen)
sin_a = M_H / nlen                       # dz per unit distance up the slope
face_plane = cq.Plane(origin=(M_L, M_W / 2, 0.0), xDir=(0, 1, 0),
                      normal=n_vec)

def fz(z):
    return z / sin_a                     # slope distance from bottom edge

def face_wp(depth):
    return cq.Workplane(face_plane).workplane(offset=-depth)

EAR_U, EAR_Z, EAR_R = 8.75, 12.0, 8.65
EYE_U, EYE_Z, EYE_R = 4.6, 8.3, 2.5
NOSE_Z, NOSE_R = 1.85, 2.0

for eu in (-EAR_U, EAR_U):
    ear = (face_wp(ENGRAVE).center(eu, fz(EAR_Z)).circle(EAR_R)
           .extrude(ENGRAVE + 1.0))
    head = head.cut(ear)
eyes = (face_wp(2 * ENGRAVE).pushPoints([(-EYE_U, fz(EYE_Z)), (EYE_U, fz(EYE_Z))])
        .circle(EYE_R).extrude(2 * ENGRAVE + 1.0))
head = head.cut(eyes)
nose = (face_wp(ENGRAVE).center(0, fz(NOSE_Z)).circle(NOSE_R)
        .extrude(ENGRAVE + 1.0))
head = head.cut(nose)

# whiskers: thin triangles, tip near the nose, wide end outward
# (u, dv) pairs relative to the nose centre, in the slanted-face plane
WHISKERS = [((3.5, 1.1), (9.1, 2.7)),     # upper whisker
            ((3.7, -0.3), (9.5, -0.65))]  # lower whisker
WHISKER_W = 1.2
nv = fz(NOSE_Z)
for s in (-1, 1):
    for (u0, v0), (u1, v1) in WHISKERS:
        dx_, dy_ = s * (u1 - u0), v1 - v0
        ln = math.hypot(dx_, dy_)
        qx, qy = -dy_ / ln * WHISKER_W / 2, dx_ / ln * WHISKER_W / 2
        p0 = (s * u0, nv + v0)
        p1 = (s * u1 + qx, nv + v1 + qy)
        p2 = (s * u1 - qx, nv + v1 - qy)
        w = (face_wp(ENGRAVE).polyline([p0, p1, p2]).close()
             .extrude(ENGRAVE + 1.0))
        head = head.cut(w)

head = head.translate((M_X0, M_Y0, M_Z0))

result = base.union(head)

VIEW = {"azimuth": 45, "elevation": 26}
